"""Angled clevis bracket.

A flat mounting plate (three holes along its straight edge, the outer two
counterbored) carries a two-lug clevis that is turned 30 deg about Z.  The lugs
have semicircular tops and a common pin bore; their outer faces are flush with
the plate's angled edges, and the slot between them has a floor that ramps up
from the open end to the plate top.
"""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
CLEVIS_ANG = -30.0     # direction of pin axis measured from +X (about Z)

BASE_T = 11.1          # mounting plate thickness
LUG_T = 9.65           # thickness of each lug
LUG_GAP = 17.3         # clear gap between the lugs
LUG_W = 33.0           # lug width (also diameter of the rounded top)
LUG_ZC = 38.85         # pin-bore centre height above plate underside
PIN_D = 17.0           # pin bore diameter
FLOOR_Z = BASE_T / 2.0 # slot floor height at the open end (ramps to BASE_T)

# plate outline; origin = outer corner of the rear lug at the open end
X_RIGHT = 60.8         # straight mounting edge
Y_TOP = 54.4
Y_BOT = -16.65
R_RIGHT = 5.3          # corner radii on the mounting edge
R_TOPLEFT = 19.8       # large blend between top edge and angled edge
R_BOTLEFT = 5.0        # blend at front corner (runs up through front lug)

# mounting holes along the straight edge
HOLE_X = 50.45
HOLE_Y_MID = 19.17
HOLE_PITCH = 24.84
HOLE_D = 9.8
CB_D = 16.6
CB_DEPTH = 1.6

H_TOTAL = LUG_ZC + LUG_W / 2.0

a = math.radians(CLEVIS_ANG)
n = (math.cos(a), math.sin(a))          # pin axis / lug thickness direction
w = (-math.sin(a), math.cos(a))         # lug width direction (along plate edge)

# ---------------- plate outline ----------------
P0 = (0.0, 0.0)                          # rear lug outer corner (sharp)
s1 = Y_BOT / n[1]
P1 = (n[0] * s1, Y_BOT)                  # open-end edge meets bottom edge
P2 = (X_RIGHT, Y_BOT)
P3 = (X_RIGHT, Y_TOP)
s4 = Y_TOP / w[1]
P4 = (w[0] * s4, Y_TOP)                  # angled edge meets top edge


def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _fillet(prev, corner, nxt, r):
    """tangent points and arc midpoint of a corner blend of radius r"""
    u1 = _unit((prev[0] - corner[0], prev[1] - corner[1]))
    u2 = _unit((nxt[0] - corner[0], nxt[1] - corner[1]))
    ang = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
    tl = r / math.tan(ang / 2.0)
    t1 = (corner[0] + u1[0] * tl, corner[1] + u1[1] * tl)
    t2 = (corner[0] + u2[0] * tl, corner[1] + u2[1] * tl)
    bis = _unit((u1[0] + u2[0], u1[1] + u2[1]))
    dc = r / math.sin(ang / 2.0)
    c = (corner[0] + bis[0] * dc, corner[1] + bis[1] * dc)
    m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
    return t1, m, t2


def outline_solid(height):
    pts = [P0, P1, P2, P3, P4]
    radii = [0.0, R_BOTLEFT, R_RIGHT, R_RIGHT, R_TOPLEFT]
    wp = cq.Workplane("XY").moveTo(*P0)
    N = len(pts)
    for i in range(1, N + 1):
        c = pts[i % N]
        r = radii[i % N]
        if r > 0:
            t1, m, t2 = _fillet(pts[i - 1], c, pts[(i + 1) % N], r)
            wp = wp.lineTo(*t1).threePointArc(m, t2)
        else:
            wp = wp.lineTo(*c)
    return wp.close().extrude(height)


plate = outline_solid(BASE_T)
envelope = outline_solid(H_TOTAL + 5.0)   # clips the lugs to the plate outline

# ---------------- clevis (built along +X, then turned) ----------------
def lug(x0):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .moveTo(0, 0).lineTo(LUG_W, 0).lineTo(LUG_W, LUG_ZC)
            .threePointArc((LUG_W / 2.0, LUG_ZC + LUG_W / 2.0), (0, LUG_ZC))
            .close().extrude(LUG_T))


lugs = lug(0.0).union(lug(LUG_T + LUG_GAP))

# pin bore (seam placed at the top of the bore)
bore_plane = cq.Plane(origin=(-5.0, LUG_W / 2.0, LUG_ZC), xDir=(0, 0, 1), normal=(1, 0, 0))
pin = cq.Workplane(bore_plane).circle(PIN_D / 2.0).extrude(2 * LUG_T + LUG_GAP + 10.0)
lugs = lugs.cut(pin)

# ramped floor of the slot between the lugs
slope = (BASE_T - FLOOR_Z) / LUG_W
ramp = (cq.Workplane("YZ", origin=(LUG_T, 0, 0))
        .polyline([(-2.0, FLOOR_Z - 2.0 * slope), (LUG_W, BASE_T),
                   (LUG_W, BASE_T + 2.0), (-2.0, BASE_T + 2.0)]).close()
        .extrude(LUG_GAP))

lugs = lugs.rotate((0, 0, 0), (0, 0, 1), CLEVIS_ANG).intersect(envelope)
ramp = ramp.rotate((0, 0, 0), (0, 0, 1), CLEVIS_ANG)

body = plate.union(lugs).cut(ramp)

# ---------------- mounting holes ----------------
hole_ys = [HOLE_Y_MID + HOLE_PITCH, HOLE_Y_MID, HOLE_Y_MID - HOLE_PITCH]
cb_pts = [(HOLE_X, hole_ys[0]), (HOLE_X, hole_ys[2])]
all_pts = [(HOLE_X, y) for y in hole_ys]

# (circle seams turned to the diagonal so they sit edge-on in the iso views)
SEAM_DIR = (1.0, 1.0, 0.0)
for (x, y) in cb_pts:
    pl = cq.Plane(origin=(x, y, BASE_T), xDir=SEAM_DIR, normal=(0, 0, 1))
    body = body.cut(cq.Workplane(pl).circle(CB_D / 2.0).extrude(-CB_DEPTH))
for (x, y) in all_pts:
    pl = cq.Plane(origin=(x, y, -1.0), xDir=SEAM_DIR, normal=(0, 0, 1))
    body = body.cut(cq.Workplane(pl).circle(HOLE_D / 2.0).extrude(BASE_T + 2.0))

result = body
